import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length along X (body, without side tongue)
D = 58.5           # overall depth along Y (body, without back tabs)
H = 24.0           # height along Z
ARM_L = 21.5       # width of the -X arm of the U
ARM_R = 20.5       # width of the +X arm of the U
BAR = 21.5         # depth of the front bar (slot bottom to front face)
SLOT_R = 5.75      # fillet radius at the inner corners of the U slot
EDGE_C = 1.0        # chamfer on the body edges

TONGUE_T = 5.5     # side tongue protrusion (on -X face)
TONGUE_H = 8.0     # tongue height (side tongue and back tabs)
TAB_T = 2.4        # back tab protrusion (on +Y faces of the arms)
TONGUE_C = 1.0     # chamfer on tongue / tab edges

VH_D = 12.4        # vertical hole diameter (through front bar)
VH_PITCH = 43.5    # spacing of the two vertical holes
VH_C = 1.3         # vertical hole countersink chamfer

HH_D = 9.0         # horizontal hole diameter (through arms, along Y)
HH_C = 1.25        # horizontal hole countersink at the front face
HH_CB_D = 11.0     # back countersink / bore diameter through the back tabs

VIEW = {"azimuth": 45, "elevation": 26}

# Coordinates: X centred on the body, front face at Y=0, back face at Y=D,
# bottom at Z=0, top at Z=H
x0, x1 = -L / 2, L / 2
zc = H / 2
sxl = x0 + ARM_L          # slot left wall
sxr = x1 - ARM_R          # slot right wall
slot_cx = (sxl + sxr) / 2  # slot centre line


def sel_edges(wp, pred):
    """Workplane holding the edges of wp's solid that satisfy pred."""
    return wp.newObject([e for e in wp.val().Edges() if pred(e)])


def is_vertical(e):
    return e.geomType() == "LINE" and abs(e.tangentAt(0.5).z) > 0.99


# ---------------- U-shaped body ----------------
pts = [(x0, 0), (x1, 0), (x1, D), (sxr, D), (sxr, BAR), (sxl, BAR), (sxl, D), (x0, D)]
body = cq.Workplane("XY").polyline(pts).close().extrude(H)

# round the two inner corners at the bottom of the slot
body = sel_edges(
    body,
    lambda e: is_vertical(e) and abs(e.Center().y - BAR) < 1e-6
    and min(abs(e.Center().x - sxl), abs(e.Center().x - sxr)) < 1e-6,
).fillet(SLOT_R)


# chamfer every remaining sharp edge (top / bottom perimeters, corner verticals)
def _sharp(e):
    c = e.Center()
    if is_vertical(e):
        # skip the tangent seams of the slot fillets
        near_fillet = (BAR - 1e-3 < c.y < BAR + SLOT_R + 1e-3) and \
            (sxl - SLOT_R - 1e-3 < c.x < sxr + SLOT_R + 1e-3)
        return not near_fillet
    if abs(e.tangentAt(0.5).z) > 0.99:
        return False
    return abs(c.z) < 1e-6 or abs(c.z - H) < 1e-6


body = sel_edges(body, _sharp).chamfer(EDGE_C)


# ---------------- tongue and back tabs ----------------
def tongue_box(xa, xb, ya, yb, za, zb, inner_axis, inner_val, c):
    """Box with chamfered edges, except the edges lying on the face that is
    buried in the body (face normal to inner_axis at coordinate inner_val)."""
    b = (cq.Workplane("XY").box(xb - xa, yb - ya, zb - za, centered=False)
         .translate((xa, ya, za)))

    def keep(e):
        cc = e.Center()
        v = getattr(cc, inner_axis)
        t = e.tangentAt(0.5)
        along = abs(getattr(t, inner_axis)) > 0.99
        return along or abs(v - inner_val) > 1e-6

    return sel_edges(b, keep).chamfer(c)


tz0, tz1 = zc - TONGUE_H / 2, zc + TONGUE_H / 2

# side tongue along the whole -X face
side = tongue_box(x0 - TONGUE_T, x0 + EDGE_C, 0, D, tz0, tz1, "x", x0 + EDGE_C, TONGUE_C)

# back tabs along the +Y faces of both arms
tab_l = tongue_box(x0, sxl, D - EDGE_C, D + TAB_T, tz0, tz1, "y", D - EDGE_C, TONGUE_C)
tab_r = tongue_box(sxr, x1, D - EDGE_C, D + TAB_T, tz0, tz1, "y", D - EDGE_C, TONGUE_C)

part = body.union(side).union(tab_l).union(tab_r)


# ---------------- holes ----------------
def revolved_tool(profile):
    """Solid of revolution about the local Z axis from an (r, z) profile."""
    return (cq.Workplane("XZ").polyline(profile).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


E = 1.0  # cutter overrun

# vertical holes through the front bar, countersunk top and bottom
r = VH_D / 2
vh_prof = [(0, -E), (r + VH_C + E, -E), (r, VH_C), (r, H - VH_C),
           (r + VH_C + E, H + E), (0, H + E)]
for sgn in (-1, 1):
    part = part.cut(revolved_tool(vh_prof)
                    .translate((slot_cx + sgn * VH_PITCH / 2, BAR / 2, 0)))

# horizontal holes along Y through each arm: countersunk at the front,
# countersunk at the back face to a larger bore that also splits the back tab
r = HH_D / 2
rb = HH_CB_D / 2
hh_prof = [(0, -E), (r + HH_C + E, -E), (r, HH_C), (r, D - (rb - r)),
           (rb, D), (rb, D + TAB_T + E), (0, D + TAB_T + E)]
for xc in (x0 + ARM_L / 2, x1 - ARM_R / 2):
    part = part.cut(revolved_tool(hh_prof)
                    .rotate((0, 0, 0), (1, 0, 0), -90)
                    .translate((xc, 0, zc)))

result = part
